import math
import cadquery as cq

# Two equal, overlapping spheres whose centres lie on the X axis,
# built as a single solid of revolution about the X axis.
R = 10.0                 # sphere radius
CENTER_DIST = 1.52 * R   # distance between sphere centres (d/D ~ 0.76)

c = CENTER_DIST / 2.0
# radius of the intersection (neck) circle at x = 0
h = math.sqrt(R * R - c * c)

# half-profile in the XY plane (y >= 0), revolved around the X axis
profile = (
    cq.Workplane("XY")
    .moveTo(-c - R, 0)
    .threePointArc((-c, R), (0, h))
    .threePointArc((c, R), (c + R, 0))
    .close()
)
body = profile.revolve(360, (0, 0, 0), (1, 0, 0))

# rotate so the revolve seam sits on the underside / back, away from view
result = body.rotate((0, 0, 0), (1, 0, 0), -45)

VIEW = {"azimuth": 45, "elevation": 26}
